"""Tetrahedral (triangular-based) pile of 20 equal balls: 10 + 6 + 3 + 1.

Bottom layer is a triangle of balls with N_BASE balls per edge, its straight
edge on the -Y side and its apex toward +Y.  Every upper layer sits in the
pockets of the layer below (close packing), so the single top ball is above
the centroid of the base triangle.
"""
import math
import cadquery as cq

# --- driving dimensions ---------------------------------------------------
R = 10.0            # ball radius
N_BASE = 4          # balls along one edge of the bottom (triangular) layer
GAP = 0.0           # extra centre spacing between neighbouring balls (0 = touching)

D = 2.0 * R + GAP                       # centre-to-centre spacing
ROW_DY = D * math.sqrt(3.0) / 2.0       # spacing of rows inside a layer (along Y)
LAYER_DZ = D * math.sqrt(2.0 / 3.0)     # vertical spacing of the layers
LAYER_SHIFT = ROW_DY / 3.0              # each layer sits over the triangular pockets

# Orientation (pole axis, seam direction) of every ball's spherical face for the
# 4-layer pile, in build order.  Purely cosmetic: it tucks each sphere's seam
# edge into the crevices between touching balls.  Other sizes use the default.
SEAM_FRAMES_4 = (
    ((0.9533, 0.0010, 0.3019), (0.1314, 0.8990, -0.4178)),
    ((0.9562, -0.0000, 0.2928), (0.0878, 0.9540, -0.2868)),
    ((0.9979, 0.0009, -0.0647), (-0.0009, 1.0000, 0.0001)),
    ((0.2493, -0.0407, -0.9676), (-0.7785, 0.5858, -0.2253)),
    ((0.4991, 0.8589, -0.1150), (0.8406, -0.4476, 0.3050)),
    ((0.8893, -0.0365, 0.4559), (0.2216, 0.9064, -0.3596)),
    ((0.0000, -0.7132, 0.7009), (-0.5615, 0.5800, 0.5902)),
    ((0.5960, 0.7969, -0.0987), (0.7555, -0.5150, 0.4049)),
    ((0.0008, -0.8952, 0.4457), (-0.9596, -0.1261, -0.2515)),
    ((0.1143, -0.4842, 0.8675), (-0.7627, -0.6023, -0.2357)),
    ((-0.9534, -0.0027, -0.3018), (0.3009, 0.0715, -0.9510)),
    ((0.9543, 0.0001, 0.2990), (0.1108, 0.9287, -0.3540)),
    ((0.5307, -0.0531, -0.8459), (-0.8113, 0.2568, -0.5252)),
    ((0.6532, 0.1744, 0.7368), (0.7539, -0.2399, -0.6116)),
    ((-0.2137, -0.1034, 0.9714), (-0.8287, -0.5074, -0.2363)),
    ((-0.0005, -0.5680, 0.8230), (-0.2124, -0.8042, -0.5551)),
    ((-0.9531, -0.0023, -0.3028), (0.3019, 0.0703, -0.9508)),
    ((0.5480, -0.0105, -0.8364), (-0.8360, 0.0264, -0.5480)),
    ((-0.0095, -0.5750, 0.8181), (-0.7684, -0.5194, -0.3740)),
    ((-0.7028, -0.7113, 0.0122), (-0.3192, 0.2999, -0.8990)),
)


def ball_centres():
    pts = []
    for k in range(N_BASE):             # layer index (0 = bottom)
        n = N_BASE - k                  # balls per edge in this layer
        z = R + k * LAYER_DZ
        for j in range(n):              # row index inside the layer (toward +Y)
            y = k * LAYER_SHIFT + j * ROW_DY
            m = n - j                   # balls in this row
            for i in range(m):
                x = (i - (m - 1) / 2.0) * D
                pts.append((x, y, z))
    return pts


def frame(idx):
    """Pole axis and seam direction (orthonormal) for ball number idx."""
    if N_BASE == 4 and idx < len(SEAM_FRAMES_4):
        p, s = SEAM_FRAMES_4[idx]
    else:
        p, s = (0.0, 0.0, 1.0), (1.0, 0.0, 0.0)
    p = cq.Vector(*p).normalized()
    s = cq.Vector(*s)
    s = (s - p * s.dot(p)).normalized()
    return p, s


pts = ball_centres()
# centre the pile on the origin in X/Y (centroid of the base triangle)
cy = (N_BASE - 1) * ROW_DY / 3.0
pts = [(x, y - cy, z) for (x, y, z) in pts]

unit_ball = cq.Solid.makeSphere(R, cq.Vector(0, 0, 0), angleDegrees1=-90, angleDegrees2=90)
balls = []
for idx, c in enumerate(pts):
    pole, seam = frame(idx)
    loc = cq.Location(cq.Plane(origin=c, xDir=seam, normal=pole))
    balls.append(unit_ball.moved(loc))

# 20 separate touching balls, kept together as one compound part
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(balls)])

VIEW = {"azimuth": 45, "elevation": 26}
